import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 62.0            # plate width  (X)
L = 100.0           # plate length (Y)
T1 = 6.0            # plate thickness
R_PLATE = 4.5       # plate corner radius (vertical edges)

# spigot frame below the plate
INS_X = 3.1         # frame inset from plate edge, X sides
INS_YN = 3.0        # frame inset at -Y end
INS_YP = 3.3        # frame inset at +Y end
C_FRAME_N = 2.7     # frame corner chamfer at -Y end
R_FRAME_BLEND = 2.0 # blend between frame chamfer and block side faces
R_FRAME_P = 1.2     # frame corner radius at +Y end
T2 = 5.2            # frame depth below plate

# underside pocket
RIM_X = 3.0         # side rim width
RIM_YP = 2.5        # +Y rim width
POCKET_INTO_PLATE = 3.3   # pocket floor height above plate underside
R_POCKET_CORNER = 2.0     # vertical corner radius of pocket
FIL_POCKET = 1.6         # fillet between pocket walls and floor

# deep block at -Y end
BLK_INS_X = 5.1
BLK_LEN = 7.7
BLK_DEPTH = 10.7

# countersunk holes
HOLE_DX = 21.4            # |x| of hole centres
HOLE_FROM_END = 21.35     # distance of holes from +Y end
HOLE_D = 6.6
CSK_D = 13.0
CSK_ANGLE = 80.0
CSK_LIP = 0.3             # short cylindrical lip above the cone
BOSS_R = 6.6              # boss around each hole on the underside

# +Y end tongue (middle section of +Y rim, thin and flush with plate end)
TAB_T = 2.0
TONGUE_W = 16.0

VIEW = {"azimuth": 45, "elevation": 26}

hole_y = L / 2 - HOLE_FROM_END
hole_pts = [(-HOLE_DX, hole_y), (HOLE_DX, hole_y)]

# ---------------- plate (z = 0 .. T1) ----------------
plate = (cq.Workplane("XY").sketch()
         .rect(W, L).vertices().fillet(R_PLATE).finalize()
         .extrude(T1))

# ---------------- spigot frame (z = -T2 .. 0) ----------------
fw = W - 2 * INS_X
fl = L - INS_YN - INS_YP
fyc = (INS_YN - INS_YP) / 2.0
frame = (cq.Workplane("XY").center(0, fyc)
         .rect(fw, fl).extrude(-T2)
         .edges("|Z and <Y").chamfer(C_FRAME_N)
         .edges("|Z and >Y").fillet(R_FRAME_P))

# ---------------- deep block at -Y end ----------------
blk = (cq.Workplane("XY")
       .center(0, -L / 2 + BLK_LEN / 2)
       .rect(W - 2 * BLK_INS_X, BLK_LEN)
       .extrude(-BLK_DEPTH))

body = plate.union(frame).union(blk)

# blend the concave vertical edges where the chamfered frame corners meet the
# block side faces
blend_sel = cq.selectors.BoxSelector(
    (-(W / 2 - BLK_INS_X) - 1.0, -L / 2 + 1.0, -T2 - 0.1),
    ((W / 2 - BLK_INS_X) + 1.0, -L / 2 + INS_YN + C_FRAME_N - 0.5, 0.1))
body = body.edges(blend_sel).edges("|Z").fillet(R_FRAME_BLEND)

# ---------------- underside pocket ----------------
px0 = -(fw / 2 - RIM_X)
px1 = fw / 2 - RIM_X
py0 = -L / 2 + BLK_LEN
py1 = L / 2 - INS_YP - RIM_YP
z_bot = -T2 - 1.0
tool_h = T2 + 1.0 + POCKET_INTO_PLATE
pocket = (cq.Workplane("XY").workplane(offset=z_bot)
          .center((px0 + px1) / 2, (py0 + py1) / 2)
          .rect(px1 - px0, py1 - py0)
          .extrude(tool_h))
bosses = (cq.Workplane("XY").workplane(offset=z_bot - 1)
          .pushPoints(hole_pts).circle(BOSS_R).extrude(tool_h + 2))
pocket = pocket.cut(bosses)
pocket = pocket.edges("|Z").fillet(R_POCKET_CORNER)
pocket = pocket.faces(">Z").edges().fillet(FIL_POCKET)
body = body.cut(pocket)

# ---------------- +Y end tongue ----------------
# middle section of the +Y rim is only TAB_T deep and runs out flush
# with the plate end
tongue_y0 = L / 2 - INS_YP - RIM_YP
tongue_len = L / 2 - tongue_y0
cut_mid = (cq.Workplane("XY").workplane(offset=-TAB_T)
           .center(0, tongue_y0 + tongue_len / 2)
           .rect(TONGUE_W, tongue_len + 0.02)
           .extrude(-T2))
body = body.cut(cut_mid)
tongue = (cq.Workplane("XY")
          .center(0, tongue_y0 + tongue_len / 2)
          .rect(TONGUE_W, tongue_len)
          .extrude(-TAB_T))
body = body.union(tongue)

# ---------------- countersunk holes from the top ----------------
body = (body.faces(">Z").workplane(origin=(0, 0, T1 - CSK_LIP))
        .pushPoints(hole_pts)
        .cskHole(HOLE_D, CSK_D, CSK_ANGLE))
lip = (cq.Workplane("XY").workplane(offset=T1 - CSK_LIP)
       .pushPoints(hole_pts).circle(CSK_D / 2).extrude(CSK_LIP + 0.01))
body = body.cut(lip)

result = body
